"""Checkerboard tile mat: an 8 x 8 grid of square tiles that alternate between a
thin and a thick tile (the thick ones stand proud of their neighbours), every
tile carrying a small blind pocket centred in its underside."""

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_X = 8                # tiles along X
N_Y = 8                # tiles along Y
TILE = 20.0            # tile pitch (tiles butt against each other, no gap)
T_LOW = 2.0            # thickness of the low tiles  ((i + j) even, incl. the -X/-Y corner)
T_HIGH = 3.0           # thickness of the high tiles ((i + j) odd)
POCKET_D = 3.4         # blind pocket in the middle of every tile underside
POCKET_DEPTH = 1.2

VIEW = {"azimuth": 45, "elevation": 26}

x0 = -N_X * TILE / 2.0
y0 = -N_Y * TILE / 2.0


def tile_thickness(i, j):
    """Checkerboard: low and high tiles alternate in both directions."""
    return T_LOW if (i + j) % 2 == 0 else T_HIGH


def make_tile(i, j):
    cx = x0 + (i + 0.5) * TILE
    cy = y0 + (j + 0.5) * TILE
    slab = (
        cq.Workplane("XY")
        .center(cx, cy)
        .rect(TILE, TILE)
        .extrude(tile_thickness(i, j))
    )
    pocket = (
        cq.Workplane("XY")
        .center(cx, cy)
        .circle(POCKET_D / 2.0)
        .extrude(POCKET_DEPTH)
    )
    return slab.cut(pocket).val()


tiles = [make_tile(i, j) for i in range(N_X) for j in range(N_Y)]

# Fuse the tiles into one body; the tile outlines stay as separate faces
# (no face merging), so every tile keeps its own top and bottom face.
mat = tiles[0].fuse(*tiles[1:], glue=False)

result = cq.Workplane("XY").add(mat)
